import math
import cadquery as cq

# =====================================================================
#  Divider tray: square box on 2x2 chamfered feet with three slanted,
#  trapezoidal divider fins. The space behind the rear fin is filled
#  up to just below the rim.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
W = 100.0            # outer box size (square)
R_OUT = 4.0          # vertical corner radius of the box
PAD_H = 5.9          # height of the bottom feet (pads)
BOX_H = 23.5         # box height from its bottom face to the rim top
FLOOR_T = 3.3        # floor thickness
R_RIM = 1.0          # outer rim top fillet
RIM_FLAT = 0.5       # flat on the rim top
LIP_CH1 = 1.0        # upper 45 deg lead-in chamfer of the lip
LIP_FACE = 1.3       # height of the vertical lip face
LIP_CH2 = 0.8        # lower 45 deg step of the lip
T_WALL = R_RIM + RIM_FLAT + LIP_CH1 + LIP_CH2   # wall thickness (3.3)

# feet
PAD_CH = 2.7         # 45 deg chamfer from the box bottom into each pad
PAD_BOT_CH = 1.1     # chamfer on the pad bottom edges
HOLE_D = 7.5         # shallow dimples in the pad bottoms
HOLE_DEPTH = 2.0
HOLE_OFF = 15.5      # dimple offset from the pad centre (both axes)

# fins (dividers)
N_FIN = 3
FIN_T = 2.7
FIN_TILT = 13.5          # lean toward +Y (deg from vertical)
FIN_TOP_ABOVE_RIM = 47.3
FIN_PITCH = 28.6
FIN_LAST_TOP_Y = 48.5    # y of the rounded top of the rear fin
FIN_HALF_AT_RIM = 40.2   # half width of the trapezoid at rim height
FIN_SLOPE = 0.355        # dx/dz of the trapezoid flanks
FIN_TOP_R = 11.5         # rounded top corners
FIN_FOOT_R = 5.5         # concave blend between flank and notch bottom
FIN_U_DROP = 3.3         # notch bottom below the rim top
FIN_EAR_DROP = 1.6       # top of the rounded ear (at the wall) below rim top
FIN_EAR_W = 1.6          # ear width out from the lip face
FIN_EAR_R = 1.3          # ear corner radius
FIN_EAR_IN_R = 0.35      # small blend at the notch / ear junction
FIN_EDGE_R = 1.3         # rounding of the fin perimeter
FIN_BASE_R = 2.5         # fillet between fins and floor

FILL_DROP = 1.2          # top of the fill behind the rear fin, below rim top

# ---------------- derived levels ----------------
Z_BOX0 = PAD_H
Z_TOP = Z_BOX0 + BOX_H
Z_FLOOR = Z_BOX0 + FLOOR_T
Z_FIN_TOP = Z_TOP + FIN_TOP_ABOVE_RIM
Z_FILL = Z_TOP - FILL_DROP

X_WALL = W / 2.0 - T_WALL            # inner face of the lower wall
X_LIP = X_WALL + LIP_CH2              # inner face of the lip
X_RIM = X_LIP + LIP_CH1               # inner edge of the rim top
Z_LIP = Z_TOP - LIP_CH1               # top of the lip face
Z_STEP = Z_LIP - LIP_FACE             # top of the lower step chamfer
Z_LOW = Z_STEP - LIP_CH2              # top of the lower wall face


def rrect(w, h, r, z0, height):
    return (cq.Workplane("XY").workplane(offset=z0)
            .sketch().rect(w, h).vertices().fillet(r).finalize()
            .extrude(height))


# ---------------- box body ----------------
body = (cq.Workplane("XY").workplane(offset=Z_BOX0)
        .rect(W, W).extrude(BOX_H)
        .edges("|Z").fillet(R_OUT)
        .faces(">Z").edges().fillet(R_RIM))

R_CAV = 1.0   # corner radius of the cavity at the lower wall
cavity = rrect(2 * X_WALL, 2 * X_WALL, R_CAV, Z_FLOOR, Z_LOW - Z_FLOOR + 0.01)
cavity = cavity.union(
    cq.Workplane("XY").workplane(offset=Z_LOW)
    .sketch().rect(2 * X_WALL, 2 * X_WALL).vertices().fillet(R_CAV).finalize()
    .extrude(LIP_CH2, taper=-45))
cavity = cavity.union(rrect(2 * X_LIP, 2 * X_LIP, R_CAV + LIP_CH2,
                            Z_STEP - 0.01, LIP_FACE + 0.02))
cavity = cavity.union(
    cq.Workplane("XY").workplane(offset=Z_LIP)
    .sketch().rect(2 * X_LIP, 2 * X_LIP).vertices().fillet(R_CAV + LIP_CH2).finalize()
    .extrude(LIP_CH1, taper=-45))
cavity = cavity.union(rrect(2 * X_RIM, 2 * X_RIM, R_CAV + LIP_CH2 + LIP_CH1,
                            Z_TOP - 0.01, 2.0))
body = body.cut(cavity)

# ---------------- feet (2 x 2 pads) ----------------
PAD_W = W / 2.0
PAD_IN = PAD_W - 2 * PAD_CH          # pad width below the 45 deg chamfer
HOLE_PTS = []
for sx in (-1, 1):
    for sy in (-1, 1):
        cx, cy = sx * PAD_W / 2.0, sy * PAD_W / 2.0
        # pad corners grow to the box corner radius at the top of the chamfer
        sk = (cq.Sketch().rect(PAD_IN, PAD_IN)
              .vertices().fillet(R_OUT - PAD_CH))
        prism = (cq.Workplane("XY").center(cx, cy).placeSketch(sk)
                 .extrude(PAD_H - PAD_CH + 0.01)
                 .faces("<Z").edges().chamfer(PAD_BOT_CH))
        sk2 = (cq.Sketch().rect(PAD_IN, PAD_IN)
               .vertices().fillet(R_OUT - PAD_CH))
        frustum = (cq.Workplane("XY").workplane(offset=Z_BOX0 - PAD_CH)
                   .center(cx, cy).placeSketch(sk2)
                   .extrude(PAD_CH, taper=-45))
        body = body.union(prism).union(frustum)
        HOLE_PTS += [(cx + a * HOLE_OFF, cy + b * HOLE_OFF)
                     for a in (-1, 1) for b in (-1, 1)]

# shallow dimples in the pad bottoms
dimples = (cq.Workplane("XY").pushPoints(HOLE_PTS)
           .circle(HOLE_D / 2.0).extrude(HOLE_DEPTH))
body = body.cut(dimples)

# ---------------- fins ----------------
ct = math.cos(math.radians(FIN_TILT))
st = math.sin(math.radians(FIN_TILT))
tt = st / ct
v_bot = -1.5                              # buried in the floor
v_top = (Z_FIN_TOP - Z_FLOOR) / ct
v_u = (Z_TOP - FIN_U_DROP - Z_FLOOR) / ct     # bottom of the notch
v_b = (Z_TOP - FIN_EAR_DROP - Z_FLOOR) / ct   # top of the ear at the wall
x_full = X_LIP + 0.3                      # buried in the side walls
x_b0 = X_LIP - FIN_EAR_W                  # inner side of the ear
x_u1 = FIN_HALF_AT_RIM + FIN_SLOPE * FIN_U_DROP
x_s1 = FIN_HALF_AT_RIM - FIN_SLOPE * (Z_FIN_TOP - Z_TOP)

# fin outline in its own (tilted) plane: x across, v up the fin
half = [(x_full, v_bot), (x_full, v_b), (x_b0, v_b), (x_b0, v_u),
        (x_u1, v_u), (x_s1, v_top)]
prof = half + [(-x, v) for (x, v) in reversed(half)]


def _yedges(f, x, v):
    return [e for e in f.Edges()
            if abs(e.Center().z - v) < 0.05 and abs(abs(e.Center().x) - x) < 0.05
            and abs(e.Center().y) < 0.05]


def make_fin():
    f = (cq.Workplane("XZ").polyline(prof).close()
         .extrude(FIN_T / 2.0, both=True).val())
    f = f.fillet(FIN_TOP_R, _yedges(f, x_s1, v_top))
    f = f.fillet(FIN_FOOT_R, _yedges(f, x_u1, v_u))
    f = f.fillet(FIN_EAR_IN_R, _yedges(f, x_b0, v_u))
    f = f.fillet(FIN_EAR_R, _yedges(f, x_b0, v_b))
    # round the exposed perimeter (top, flanks, notch, ears)
    ed = [e for e in f.Edges()
          if abs(abs(e.Center().y) - FIN_T / 2.0) < 0.01
          and e.Center().z > v_u - 0.05]
    return f.fillet(FIN_EDGE_R, ed)


fin0 = make_fin()
FIN_PIVOTS = []
for k in range(N_FIN):
    y_top = FIN_LAST_TOP_Y - (N_FIN - 1 - k) * FIN_PITCH
    y_piv = y_top - (v_top - FIN_T / 2.0) * st
    fk = fin0.rotate(cq.Vector(0, 0, 0), cq.Vector(1, 0, 0), -FIN_TILT)
    fk = fk.translate(cq.Vector(0, y_piv, Z_FLOOR))
    body = body.union(cq.Workplane("XY").add(fk))
    FIN_PIVOTS.append(y_piv)

# ---------------- fill behind the rear fin ----------------
y_c_bot = FIN_PIVOTS[-1] - 0.5 * tt
y_c_top = FIN_PIVOTS[-1] + (Z_FILL - Z_FLOOR) * tt
x_fill = X_LIP + 0.3
fill = (cq.Workplane("YZ", origin=(-x_fill, 0, 0))
        .polyline([(y_c_bot, Z_FLOOR - 0.5), (X_LIP + 0.3, Z_FLOOR - 0.5),
                   (X_LIP + 0.3, Z_FILL), (y_c_top, Z_FILL)]).close()
        .extrude(2 * x_fill))
body = body.union(fill)

# ---------------- blend the fins into the floor ----------------
solid = body.val()
base_edges = []
for e in solid.Edges():
    c = e.Center()
    if abs(c.z - Z_FLOOR) > 0.05 or e.Length() < 60:
        continue
    if any(abs(c.y - yp) < FIN_T for yp in FIN_PIVOTS):
        base_edges.append(e)
if base_edges:
    solid = solid.fillet(FIN_BASE_R, base_edges)

result = cq.Workplane("XY").add(solid)
